import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Flat sheet-metal mounting plate (laser cut), 1.0 mm thick.
# All plan dimensions in mm, origin at lower-left corner of the bounding box,
# the finished part is re-centred on the origin at the end.
# ---------------------------------------------------------------------------

T = 1.0            # sheet thickness
W = 284.5          # overall width  (X)
H = 197.9          # overall depth  (Y)

# main outline levels
Y_STRIP = 35.0     # top edge of the front (lower) strip
Y_UPPER = 127.7    # lower edge of the rear-left section
Y_MID = 172.0      # rear edge between the two rear sections
X_STEP = 138.2     # right end of the rear-left section
X_RSEC = 221.0     # left end of the rear-right section
Y_RTOP = 195.1     # rear edge of the rear-right section
R_STEP = 7.0       # fillet in the inner corner of the rear-right section
RELIEF_R = 5.5     # relief round at the inner corner of the rear-left section
BAR_X0, BAR_X1 = 122.0, 130.0   # thin connecting bar

# corner notches
N_TL = (11.2, 183.4)   # (x, y) inner corner of top-left notch
N_TR = (272.5, 183.0)
N_BR = (272.2, 8.3)
N_BL = (11.2, 8.3)
R_NOTCH_T = 8.5   # rear corner notches
R_NOTCH_F = 7.5   # front corner notches

# front-right opening
OPEN_X0, OPEN_X1, OPEN_Y = 238.2, 267.2, 39.1
# small notch in the front edge
SN_X, SN_W, SN_D = 228.7, 4.0, 3.7

# locating tab on the rear-left section
TAB_X0, TAB_X1, TAB_Y = 27.5, 36.5, 111.5

# big central window
WIN_X0, WIN_X1 = BAR_X1, 212.4
WIN_Y0 = Y_STRIP
WIN_YT_L, WIN_YT_R = Y_UPPER, 129.5
WIN_N_X0, WIN_N_X1, WIN_N_Y = 175.7, 187.4, 147.0

HOLE_D = 4.0
PILOT_D = 2.0
BIG_HOLE_D = 12.0


def rounded_outline(pts, radii):
    """Closed polyline with an optional fillet radius at every vertex.
    Returns a Workplane holding one closed wire (lines + arcs)."""
    n = len(pts)
    segs = []  # list of (T1, M, T2) or (P,) per vertex
    for i in range(n):
        p = pts[i]
        r = radii[i]
        if r <= 0:
            segs.append((p,))
            continue
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        d1 = (p[0] - a[0], p[1] - a[1])
        l1 = math.hypot(*d1)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (b[0] - p[0], b[1] - p[1])
        l2 = math.hypot(*d2)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosang = -(d1[0] * d2[0] + d1[1] * d2[1])
        theta = math.acos(max(-1.0, min(1.0, cosang)))
        L = r / math.tan(theta / 2.0)
        t1 = (p[0] - d1[0] * L, p[1] - d1[1] * L)
        t2 = (p[0] + d2[0] * L, p[1] + d2[1] * L)
        cross = d1[0] * d2[1] - d1[1] * d2[0]
        nrm = (-d1[1], d1[0]) if cross > 0 else (d1[1], -d1[0])
        c = (t1[0] + nrm[0] * r, t1[1] + nrm[1] * r)
        v = (p[0] - c[0], p[1] - c[1])
        lv = math.hypot(*v)
        m = (c[0] + v[0] / lv * r, c[1] + v[1] / lv * r)
        segs.append((t1, m, t2))
    start = segs[0][-1]
    wp = cq.Workplane("XY").moveTo(*start)
    cur = start
    items = segs[1:] + [segs[0]]
    for k, s in enumerate(items):
        last = k == len(items) - 1
        if len(s) == 1:
            if not last and math.hypot(s[0][0] - cur[0], s[0][1] - cur[1]) > 1e-6:
                wp = wp.lineTo(*s[0])
                cur = s[0]
        else:
            if math.hypot(s[0][0] - cur[0], s[0][1] - cur[1]) > 1e-6:
                wp = wp.lineTo(*s[0])
            wp = wp.threePointArc(s[1], s[2])
            cur = s[2]
    return wp.close()


# ---------------------------------------------------------------- outline
outline = [
    ((N_BL[0], 0.0), 0),
    ((SN_X - SN_W / 2, 0.0), 0.5),
    ((SN_X - SN_W / 2, SN_D), 1.0),
    ((SN_X + SN_W / 2, SN_D), 1.0),
    ((SN_X + SN_W / 2, 0.0), 0.5),
    ((OPEN_X0, 0.0), 1.0),
    ((OPEN_X0, OPEN_Y), 1.2),
    ((OPEN_X1, OPEN_Y), 1.2),
    ((OPEN_X1, 0.0), 1.0),
    ((N_BR[0], 0.0), 0),
    ((N_BR[0], N_BR[1]), R_NOTCH_F),
    ((W, N_BR[1]), 0),
    ((W, N_TR[1]), 0),
    ((N_TR[0], N_TR[1]), R_NOTCH_T),
    ((N_TR[0], Y_RTOP), 0),
    ((X_RSEC, Y_RTOP), 1.0),
    ((X_RSEC, Y_MID), R_STEP),
    ((X_STEP, Y_MID), 0),
    ((X_STEP, H), 1.0),
    ((N_TL[0], H), 0),
    ((N_TL[0], N_TL[1]), R_NOTCH_T),
    ((0.0, N_TL[1]), 0),
    ((0.0, Y_UPPER), 0),
    ((TAB_X0, Y_UPPER), 1.0),
    ((TAB_X0, TAB_Y), (TAB_X1 - TAB_X0) / 2),
    ((TAB_X1, TAB_Y), (TAB_X1 - TAB_X0) / 2),
    ((TAB_X1, Y_UPPER), 1.0),
    ((BAR_X0, Y_UPPER), 1.0),
    ((BAR_X0, Y_STRIP), 1.0),
    ((0.0, Y_STRIP), 0),
    ((0.0, N_BL[1]), 0),
    ((N_BL[0], N_BL[1]), R_NOTCH_F),
]
plate = rounded_outline([p for p, r in outline], [r for p, r in outline]).extrude(T)

# ear on the front strip (half-round lug around a hole)
EAR = (72.6, Y_STRIP)
EAR_R = 3.8
plate = plate.union(
    cq.Workplane("XY").center(*EAR).circle(EAR_R).extrude(T)
)

# ---------------------------------------------------------------- cut-outs
def cut_profile(body, pts_r):
    prof = rounded_outline([p for p, r in pts_r], [r for p, r in pts_r]).extrude(T * 3).translate((0, 0, -T))
    return body.cut(prof)


# big central window with a key notch
win = [
    ((WIN_X0, WIN_Y0), 1.0),
    ((WIN_X1, WIN_Y0), 1.0),
    ((WIN_X1, WIN_YT_R), 1.0),
    ((WIN_N_X1, WIN_YT_R), 1.5),
    ((WIN_N_X1, WIN_N_Y), 1.5),
    ((WIN_N_X0, WIN_N_Y), 1.5),
    ((WIN_N_X0, WIN_YT_L), 0),
    ((WIN_X0, WIN_YT_L), 1.0),
]
plate = cut_profile(plate, win)


def rect_pts(cx, cy, w, h, r):
    return [
        ((cx - w / 2, cy - h / 2), r),
        ((cx + w / 2, cy - h / 2), r),
        ((cx + w / 2, cy + h / 2), r),
        ((cx - w / 2, cy + h / 2), r),
    ]


# rectangular windows
for (cx, cy, w, h) in [
    (42.85, 152.65, 30.7, 25.7),
    (103.0, 152.65, 30.6, 25.5),
    (252.4, 83.6, 28.9, 39.7),
]:
    plate = cut_profile(plate, rect_pts(cx, cy, w, h, 2.0))

# corner relief at the inner step corner (round almost tangent to the rear edge)
plate = plate.cut(
    cq.Workplane("XY")
    .center(X_STEP + 2.8, Y_MID + RELIEF_R - 0.3)
    .circle(RELIEF_R)
    .extrude(T * 3)
    .translate((0, 0, -T))
)

# ---------------------------------------------------------------- holes
holes = [
    (22.2, 190.9), (56.5, 190.9), (91.3, 190.9), (134.4, 190.9),
    (8.8, 177.1), (22.2, 179.8), (56.5, 179.8), (91.4, 179.8),
    (133.1, 157.2), (182.6, 157.2),
    (225.1, 190.8), (269.9, 190.9),
    (215.2, 167.2), (269.9, 160.2), (228.0, 149.3),
    (126.25, 77.8),
    (9.0, 13.7), (132.8, 14.5), (182.8, 14.5),
    (13.1, 157.9), (169.3, 135.4), (169.2, 4.4), (13.6, 4.1),
    (32.2, 115.6),          # tab hole
    EAR,                    # ear hole
]
pilots = [(13.1, 162.7), (169.3, 140.0), (169.2, 9.5), (13.2, 9.7)]

cutter = cq.Workplane("XY").pushPoints(holes).circle(HOLE_D / 2).extrude(T * 3)
cutter = cutter.union(cq.Workplane("XY").pushPoints(pilots).circle(PILOT_D / 2).extrude(T * 3))
cutter = cutter.union(cq.Workplane("XY").center(157.7, 23.4).circle(BIG_HOLE_D / 2).extrude(T * 3))
plate = plate.cut(cutter.translate((0, 0, -T)))

# ---------------------------------------------------------------- slots
slots = [
    # (cx, cy, length, width, angle)
    (123.1, 179.8, 13.8, 3.8, 0),
    (218.2, 130.9, 10.8, 3.8, 90),
    (217.9, 15.7, 14.8, 4.0, 90),
    (221.9, 119.5, 5.2, 1.8, 0),
    (221.9, 53.3, 5.2, 1.8, 0),
]
for (cx, cy, ln, wd, ang) in slots:
    plate = plate.cut(
        cq.Workplane("XY").center(cx, cy).slot2D(ln, wd, ang).extrude(T * 3).translate((0, 0, -T))
    )

# ---------------------------------------------------------------- marking
# "1.0" gauge marking, laser cut through the sheet (stencil style zero)
TXT_X, TXT_Y = 252.1, 129.15     # centre of the marking
TXT_H = 9.0                     # character height
TXT_S = 1.5                     # stroke width


def through(wp2d):
    return wp2d.extrude(T * 3).translate((0, 0, -T))


mark = through(
    cq.Workplane("XY").center(TXT_X - 4.3, TXT_Y).rect(TXT_S, TXT_H)
)
# flag of the "1"
flag_len = 3.2
mark = mark.union(
    through(
        cq.Workplane("XY")
        .center(TXT_X - 5.6, TXT_Y + TXT_H / 2 - 1.5)
        .transformed(rotate=(0, 0, 35))
        .rect(flag_len, TXT_S)
    )
)
# decimal point
mark = mark.union(
    through(cq.Workplane("XY").center(TXT_X - 1.6, TXT_Y - TXT_H / 2 + TXT_S / 2).rect(TXT_S, TXT_S))
)
# the zero: elliptic ring split by two bridges so the centre stays attached
ZX = TXT_X + 4.1
Z_A = 3.4                       # outer semi-width of the zero
ring = through(cq.Workplane("XY").center(ZX, TXT_Y).ellipse(Z_A, TXT_H / 2)).cut(
    through(cq.Workplane("XY").center(ZX, TXT_Y).ellipse(Z_A - TXT_S, TXT_H / 2 - TXT_S))
)
ring = ring.cut(through(cq.Workplane("XY").center(ZX, TXT_Y).rect(0.8, TXT_H + 2)))
mark = mark.union(ring)
plate = plate.cut(mark)

result = plate.translate((-W / 2, -H / 2, 0))
